import cadquery as cq
import math

# ---------------- overall block ----------------
L_X = 7.0     # width (X)
L_Y = 10.0    # length (Y)
H_Z = 6.0     # height (Z)

# rebate (step) along the -X bottom edge, full length
STEP_X = 2.0
STEP_Z = 2.0

# ---------------- top key: C-shaped island inside a through slot ----------------
SLOT_X0, SLOT_X1 = 1.0, 5.0      # slot outer boundary
SLOT_Y0, SLOT_Y1 = 1.0, 9.0
GAP = 0.4                        # slot width around the key
NOTCH_X1 = 3.0                   # inner edge of the key notch
NOTCH_Y0, NOTCH_Y1 = 3.4, 6.6    # notch extent along Y
KEY_BOT = 2.0                    # underside of the key (= open cavity height)
TONGUE_TOP = 5.2                 # bridge (tongue) top surface, 0.8 below the top
TONGUE_BOT = 4.4                 # bridge underside

# ---------------- pentagonal pyramid markers ----------------
PYR_R = 0.4                      # circumradius of the pentagon base
PYR_H = 0.8                      # height
PYR_EMBED = 0.05                 # apex sunk into the mating face so it fuses
SIDE_PYR_Y, SIDE_PYR_Z = 5.0, 1.0
STEP_PYR_YS = (2.5, 7.5)

# fine scribed line on the +X face
LINE_Y0, LINE_Y1, LINE_Z = 5.38, 9.0, 1.0
LINE_W = 0.025


def pent_pyramid(apex, axis, ref, r=PYR_R, h=PYR_H):
    """Pentagonal pyramid, apex at `apex`, axis = base->apex direction, first base vertex toward `ref`."""
    ax = cq.Vector(*axis).normalized()
    base_c = cq.Vector(*apex) - ax * h
    rv = cq.Vector(*ref)
    u = (rv - ax * rv.dot(ax)).normalized()
    v = ax.cross(u)
    pts = [base_c + u * (r * math.cos(2 * math.pi * k / 5)) + v * (r * math.sin(2 * math.pi * k / 5))
           for k in range(5)]
    apex_v = cq.Vector(*apex)
    faces = [cq.Face.makeFromWires(cq.Wire.makePolygon(pts + [pts[0]]))]
    for k in range(5):
        faces.append(cq.Face.makeFromWires(cq.Wire.makePolygon([pts[k], pts[(k + 1) % 5], apex_v, pts[k]])))
    return cq.Workplane().add(cq.Solid.makeSolid(cq.Shell.makeShell(faces)))


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


# main block with the rebate
body = box(0, L_X, 0, L_Y, 0, H_Z).cut(box(0, STEP_X, 0, L_Y, -1, STEP_Z))

# open cavity under the key (bottom side, open into the rebate)
body = body.cut(box(SLOT_X0, SLOT_X1, SLOT_Y0, SLOT_Y1, -1, KEY_BOT))

# through slot loop separating the C-shaped key, leaving the tongue as a bridge
outer = box(SLOT_X0, SLOT_X1, SLOT_Y0, SLOT_Y1, -1, H_Z + 1)
key = box(SLOT_X0 + GAP, SLOT_X1 - GAP, SLOT_Y0 + GAP, SLOT_Y1 - GAP, -2, H_Z + 2)
key = key.cut(box(SLOT_X0 - 1, NOTCH_X1, NOTCH_Y0, NOTCH_Y1, -3, H_Z + 3))
tongue = box(SLOT_X0 - 1, NOTCH_X1, NOTCH_Y0 + GAP, NOTCH_Y1 - GAP, -3, H_Z + 3)
body = body.cut(outer.cut(key).cut(tongue))

# notch pocket above the tongue and clearance below it
body = body.cut(box(SLOT_X0, NOTCH_X1, NOTCH_Y0, NOTCH_Y1, TONGUE_TOP, H_Z + 1))
body = body.cut(box(SLOT_X0, NOTCH_X1, NOTCH_Y0, NOTCH_Y1, -1, TONGUE_BOT))

# scribed line on the +X face
body = body.cut(box(L_X - LINE_W, L_X + 1, LINE_Y0, LINE_Y1, LINE_Z - LINE_W / 2, LINE_Z + LINE_W / 2))

# pyramid markers: one on the +X face (apex on the face), two under the key at the rebate wall
body = body.union(pent_pyramid((L_X - PYR_EMBED, SIDE_PYR_Y, SIDE_PYR_Z), (-1, 0, 0), (0, 0, 1), h=PYR_H + PYR_EMBED))
for py in STEP_PYR_YS:
    body = body.union(pent_pyramid((STEP_X, py, KEY_BOT + PYR_EMBED), (0, 0, 1), (1, 0, 0), h=PYR_H + PYR_EMBED))

result = body.translate((-L_X / 2, -L_Y / 2, 0))
